import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------------------
TUBE_SPACING = 254.0      # Y distance between the two duct axes
R_REAR = 137.0            # rear duct section radius
R_FRONT = 141.0           # front duct section radius
X_REAR = -220.0           # rear end of body
X_STEP = 90.0             # radius step position
X_FRONT = 220.0           # front end of body
FLANGE_R = 141.0          # end flange outer radius
FLANGE_T = 14.0           # end flange thickness
BORE_APO = 86.0           # octagonal bore apothem (through, mid section)
MOUTH_APO = 118.0         # octagonal mouth apothem at the duct ends
MOUTH_APO2 = 106.0        # mouth apothem at the inner end of the mouth
MOUTH_DEPTH = 110.0       # depth of the tapered mouth
REAR_HOLE_R = 97.0        # round openings in the rear flange plate
DECK_Z = 140.0            # flat deck height between ducts (rear section)
CHAMF_Z = 80.0            # height where side chamfer meets the rear duct

# drum head
DRUM_TILT = 26.0          # deg, axis tilt (front end up)
FACE_C = (62.0, 0.0, 350.0)   # centre of the drum face
DRUM_R = 124.0            # radius at the face end
DRUM_R_TAPER = 0.0   # radius loss per mm toward the rear
DRUM_WALL = 8.0
DRUM_BASE_Z = 212.0       # drum is trimmed flat here (sits on the cradle)
REAR_PT = (-298.0, 326.0) # (x, z) point on the oblique rear rim plane
REAR_ANG = 37.0           # rear rim plane angle from vertical (deg)
FACE_R = 134.0            # 16-gon face plate circumradius
FACE_T = 26.0
FACE_OPEN_R = 84.0

# cradle / lugs
RAIL_Y = 144.0
RAIL_W = 24.0
RAIL_TOP = 214.0
LUG_Y = 211.0
LUG_W = 74.0
FOOT_Z = -236.0           # bottom of the feet

# tubes of guards
TUBE_R = 20.0

Y0 = TUBE_SPACING / 2.0


def poly_pts(n, r, rot=0.0, cx=0.0, cy=0.0):
    return [(cx + r * math.cos(math.radians(rot + 360.0 * i / n)),
             cy + r * math.sin(math.radians(rot + 360.0 * i / n))) for i in range(n)]


def yz_wp(x):
    return cq.Workplane("YZ", origin=(x, 0, 0))


TUBE_SIDES = 8            # guard tubes are faceted (octagonal) sections


def ngon_wire(r, p0, t0, n):
    ref = cq.Vector(0, 0, 1) if abs(t0.z) < 0.9 else cq.Vector(1, 0, 0)
    u = ref.cross(t0).normalized()
    v = t0.cross(u).normalized()
    pts = []
    for i in range(n):
        a = 2 * math.pi * (i + 0.5) / n
        pts.append(p0 + u * (r * math.cos(a)) + v * (r * math.sin(a)))
    return cq.Wire.makePolygon(pts, close=True)


def pipe(pts, r=TUBE_R, bend=75.0, bore=0.0):
    w = cq.Wire.makePolygon([cq.Vector(*p) for p in pts])
    if len(pts) > 2:
        w = w.fillet(bend)
    t0 = w.tangentAt(0)
    p0 = w.startPoint()
    prof = ngon_wire(r, p0, t0, TUBE_SIDES)
    inner = [cq.Wire.makeCircle(bore, p0, t0)] if bore > 0 else []
    s = cq.Solid.sweep(prof, inner, w, True, False, None, "right")
    return cq.Workplane("XY").add(s)


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def twin(x0, r, length):
    a = yz_wp(x0).center(-Y0, 0).circle(r).extrude(length)
    b = yz_wp(x0).center(Y0, 0).circle(r).extrude(length)
    return a.union(b)


def xz_prism(pts, y0, y1):
    """Polygon in the XZ plane (x, z) extruded from y0 to y1."""
    return (cq.Workplane("XZ", origin=(0, y1, 0)).polyline(pts).close()
            .extrude(y1 - y0))


# ---------------------------------------------------------------------------
# Body: twin ducts
# ---------------------------------------------------------------------------
rear_len = X_STEP - X_REAR
rear = twin(X_REAR, R_REAR, rear_len)
rear = rear.union(box(X_REAR, X_STEP, -Y0, Y0, 0, DECK_Z))
# chamfer planes on the upper outer sides of the rear section; the chamfer
# rises slightly toward the front (ruled two-section loft)


def clip_profile(cz, top):
    yc_ = Y0 + math.sqrt(R_REAR ** 2 - cz ** 2)
    yt_ = Y0 + 22.0
    sl = (top - cz) / (yc_ - yt_)
    zf = cz - (400 - yc_) * sl
    return [(-400, -400), (400, -400), (400, zf), (yc_, cz),
            (yt_, top), (-yt_, top), (-yc_, cz), (-400, zf)]


clip = (yz_wp(X_REAR - 1).polyline(clip_profile(CHAMF_Z - 8, DECK_Z)).close()
        .workplane(offset=rear_len + 2)
        .polyline(clip_profile(CHAMF_Z + 14, DECK_Z + 4)).close()
        .loft(ruled=True))
rear = rear.intersect(clip)

front = twin(X_STEP, R_FRONT, X_FRONT - FLANGE_T - X_STEP)


def flange(x0, r):
    f = twin(x0, r, FLANGE_T)
    tab = yz_wp(x0).pushPoints([(0, 86), (0, -86)]).rect(46, 44).extrude(FLANGE_T)
    return f.union(tab)


fl_front = flange(X_FRONT - FLANGE_T, FLANGE_R)
try:
    fl_front = fl_front.faces(">X").edges().fillet(7.0)
except Exception:
    pass
fl_rear = flange(X_REAR, FLANGE_R - 4)
body = rear.union(front).union(fl_front).union(fl_rear)

# bottom web between the ducts with a window
body = body.union(box(-160, 170, -70, 70, -128, -60))
body = body.cut(box(-70, 50, -48, 48, -140, -50))

# octagonal through bores with gently tapered octagonal mouths at both ends
bore_r = BORE_APO / math.cos(math.radians(22.5))
mouth_r = MOUTH_APO / math.cos(math.radians(22.5))
mouth_r2 = MOUTH_APO2 / math.cos(math.radians(22.5))
cutters = []
for yy in (-Y0, Y0):
    pts = poly_pts(8, bore_r, 22.5, yy, 0)
    cutters.append(yz_wp(X_REAR - 5).polyline(pts).close()
                   .extrude(X_FRONT - X_REAR + 10).val())
    mouth = (yz_wp(X_FRONT + 1).polyline(poly_pts(8, mouth_r, 22.5, yy, 0)).close()
             .workplane(offset=-MOUTH_DEPTH)
             .polyline(poly_pts(8, mouth_r2, 22.5, yy, 0)).close()
             .loft(ruled=True))
    cutters.append(mouth.val())
    # rear: round opening through the rear flange plate, then the bore
    cutters.append(yz_wp(X_REAR - 1).center(yy, 0).circle(REAR_HOLE_R)
                   .extrude(FLANGE_T + 2).val())
cutter = cq.Workplane("XY").add(cutters[0])
for c in cutters[1:]:
    cutter = cutter.union(cq.Workplane("XY").add(c))
body = body.cut(cutter)

# bolt holes on the flanges
bolt_pts = []
for yy in (-Y0, Y0):
    for k in range(12):
        a = 90 + 30 * k
        py = yy + 133 * math.cos(math.radians(a))
        pz = 133 * math.sin(math.radians(a))
        if abs(py) < 45:
            continue
        bolt_pts.append((py, pz))
bolt_pts += [(0, 92), (0, -92)]
body = body.cut(yz_wp(X_FRONT - FLANGE_T - 1).pushPoints(bolt_pts).circle(4.5)
                .extrude(FLANGE_T + 2))
rear_bolts = []
for yy in (-Y0, Y0):
    for k in range(10):
        a = 90 + 36 * k
        py = yy + 116 * math.cos(math.radians(a))
        pz = 116 * math.sin(math.radians(a))
        if abs(py) < 30:
            continue
        rear_bolts.append((py, pz))
body = body.cut(yz_wp(X_REAR - 1).pushPoints(rear_bolts).circle(5)
                .extrude(FLANGE_T + 2))

# ---------------------------------------------------------------------------
# Drum head: tilted 16-sided drum, built along local +Z (face at local z = 0,
# drum extending toward local -Z), then rotated/placed; open at the rear,
# trimmed flat underneath where it sits in the cradle.
# ---------------------------------------------------------------------------
LONG = 480.0


def place(wp):
    return (wp.rotate((0, 0, 0), (0, 1, 0), 90.0 - DRUM_TILT).translate(FACE_C))


R_END = DRUM_R - DRUM_R_TAPER * LONG


DRUM_SIDES = 16


def cone(r_face, r_end):
    """Faceted (16-gon) frustum; radii are apothems, face at z=0."""
    k = 1.0 / math.cos(math.pi / DRUM_SIDES)
    rot = 180.0 / DRUM_SIDES
    return (cq.Workplane("XY").polyline(poly_pts(DRUM_SIDES, r_face * k, rot)).close()
            .workplane(offset=-LONG)
            .polyline(poly_pts(DRUM_SIDES, r_end * k, rot)).close()
            .loft(ruled=True))


outer = cone(DRUM_R, R_END)
inner = cone(DRUM_R - DRUM_WALL, R_END - DRUM_WALL).translate((0, 0, -1))
inner = inner.union(cq.Workplane("XY")
                    .polyline(poly_pts(DRUM_SIDES, DRUM_R - DRUM_WALL - 1, 180.0 / DRUM_SIDES))
                    .close().extrude(12).translate((0, 0, -2)))
shell = outer.cut(inner)
# side slots (local -X is world "up"; skip the underside)
slot_t = -112.0
slot_proto = (cq.Workplane("XY").box(40, 14, 88).edges("|X").fillet(6.5)
              .translate((DRUM_R + DRUM_R_TAPER * slot_t - 4, 0, slot_t)).val())
slot_solids = [slot_proto.rotate(cq.Vector(0, 0, 0), cq.Vector(0, 0, 1),
                                 180 + (k - 4) * 22.5) for k in range(9)]
shell = shell.cut(cq.Workplane("XY").add(cq.Compound.makeCompound(slot_solids)))

# face plate: 16-gon with ring of slots and holes
face = (cq.Workplane("XY").workplane(offset=-FACE_T)
        .polyline(poly_pts(16, FACE_R, 11.25)).close().extrude(FACE_T))
face = face.cut(cq.Workplane("XY").workplane(offset=-FACE_T - 1)
                .polyline(poly_pts(10, FACE_OPEN_R, 18)).close().extrude(FACE_T + 2))
ring_r = 106.0
slot_list = []
for k in range(8):
    pc = 180 + 45 * k
    for s_ in (-11.0, 11.0):
        a = pc + s_
        sl = (cq.Workplane("XY").box(24, 11, FACE_T + 4)
              .rotate((0, 0, 0), (0, 0, 1), a)
              .translate((ring_r * math.cos(math.radians(a)),
                          ring_r * math.sin(math.radians(a)), -FACE_T / 2)))
        slot_list.append(sl.val())
face = face.cut(cq.Workplane("XY").add(cq.Compound.makeCompound(slot_list)))
hole_pts = [(ring_r * math.cos(math.radians(180 + 22.5 + 45 * k)),
             ring_r * math.sin(math.radians(180 + 22.5 + 45 * k))) for k in range(8)]
face = face.cut(cq.Workplane("XY").workplane(offset=-FACE_T - 1)
                .pushPoints(hole_pts).rect(13, 5).extrude(FACE_T + 2))
face = face.cut(cq.Workplane("XY").workplane(offset=-FACE_T - 1)
                .pushPoints(hole_pts).rect(5, 13).extrude(FACE_T + 2))
dot_pts = []
for k in range(8):
    a = 180 + 45 * k
    dot_pts.append((121 * math.cos(math.radians(a)), 121 * math.sin(math.radians(a))))
    for s in (-17, 17):
        b = a + s
        dot_pts.append((120 * math.cos(math.radians(b)), 120 * math.sin(math.radians(b))))
face = face.cut(cq.Workplane("XY").workplane(offset=-FACE_T - 1)
                .pushPoints(dot_pts).circle(2.5).extrude(FACE_T + 2))
# support block under the lower part of the face plate (hugs the saddle)
shoulder = (cq.Workplane("XY").box(80, 236, 70)
            .translate((105, 0, -FACE_T - 35)))
drum_local = shell.union(face).union(shoulder)
drum = place(drum_local)
rim_outer = place(cone(DRUM_R + 12, R_END + 12).cut(
    cone(DRUM_R - DRUM_WALL, R_END - DRUM_WALL).translate((0, 0, -1))))

# oblique rear trim: keep the side of the plane toward +X


def half_space(offset, keep_positive=True, thick=1500.0):
    """Slab on one side of the oblique rear plane shifted by offset."""
    b = cq.Workplane("XY").box(thick, 3000, 3000)
    shift = thick / 2.0 if keep_positive else -thick / 2.0
    b = b.translate((shift + offset, 0, 0))
    b = b.rotate((0, 0, 0), (0, 1, 0), -REAR_ANG)
    return b.translate((REAR_PT[0], 0, REAR_PT[1]))


keep = half_space(0.0).intersect(box(-2000, 2000, -2000, 2000, DRUM_BASE_Z, 2000))
drum = drum.intersect(keep)
rim = (rim_outer
       .intersect(half_space(0.0).intersect(half_space(12.0, False)))
       .intersect(box(-2000, 2000, -2000, 2000, DRUM_BASE_Z, 2000)))
drum = drum.union(rim)

# ---------------------------------------------------------------------------
# Cradle / saddle on top of the body
# ---------------------------------------------------------------------------
rails = None
for sgn in (-1, 1):
    y0r, y1r = sgn * RAIL_Y - RAIL_W / 2, sgn * RAIL_Y + RAIL_W / 2
    r = xz_prism([(-225, DECK_Z - 2), (142, DECK_Z - 2), (142, 160),
                  (114, RAIL_TOP), (-225, RAIL_TOP)], y0r, y1r)
    # inclined upper outer face
    try:
        r = r.edges("|X and >Z and %s" % (">Y" if sgn > 0 else "<Y")).chamfer(16)
    except Exception:
        pass
    yo = sgn * (RAIL_Y + RAIL_W / 2)
    # slot through the inclined face
    sl = (cq.Workplane("XY").box(226, 10, 30).edges("|Z").fillet(4.9)
          .rotate((0, 0, 0), (1, 0, 0), -sgn * 45.0)
          .translate((-8, yo - sgn * 8, RAIL_TOP - 8)))
    r = r.cut(sl)
    # lower slot and hole row on the vertical outer face
    sl2 = (cq.Workplane("XY").box(226, 14, 9).edges("|Y").fillet(4.4)
           .translate((-12, yo, 160)))
    r = r.cut(sl2)
    hpts = ([(hx, 176) for hx in range(-100, 101, 50)]
            + [(hx + 25, 148) for hx in range(-100, 101, 50)])
    r = r.cut(cq.Workplane("XZ", origin=(0, yo, 0)).pushPoints(hpts)
              .circle(3).extrude(8, both=True))
    rails = r if rails is None else rails.union(r)

# base plate of the cradle (drum rests on it)
cradle = box(-215, 60, -RAIL_Y + 14, RAIL_Y - 14, DRUM_BASE_Z - 12, DRUM_BASE_Z + 1)

# saddle bridge under the drum face, legs down to the ducts
SAD_Y = RAIL_Y + RAIL_W / 2      # saddle flush with the rail outer faces
saddle = box(56, 128, -SAD_Y, SAD_Y, 179, 213)
for sgn in (-1, 1):
    ya_, yb_ = sorted((sgn * 118, sgn * SAD_Y))
    saddle = saddle.union(box(70, 128, ya_, yb_, 105, 213))
saddle = saddle.faces(">X").edges("|Y").chamfer(14)

# lifting lugs at the rear top corners
lugs = None
for sgn in (-1, 1):
    ya, yb = sgn * LUG_Y - LUG_W / 2, sgn * LUG_Y + LUG_W / 2
    yo0, yo1 = sorted((sgn * (LUG_Y - 37), sgn * (LUG_Y + 46)))
    ped = box(-210, -104, yo0, yo1, 96, 141)
    yc0, yc1 = sorted((sgn * (LUG_Y + 8), sgn * (LUG_Y + 46)))
    cb = box(-208, -172, yc0, yc1, 140, 172)
    try:
        cb = cb.faces(">Z").edges().chamfer(4)
    except Exception:
        pass
    cb = cb.cut(cq.Workplane("XY").circle(6).extrude(40)
                .translate((-190, sgn * (LUG_Y + 27), 150)))
    ped = ped.union(cb)
    wedge = xz_prism([(-172, 140), (-98, 140), (-172, 264)], ya, yb)
    # hollow the wedge into a channel: side plates, back plate, base plate
    inner_w = xz_prism([(-160, 152), (-60, 152), (-60, 400), (-160, 400)],
                       ya + 10, yb - 10)
    wedge = wedge.cut(inner_w)
    lug = ped.union(wedge)
    lug = lug.cut(cq.Workplane("XY").circle(9).extrude(60)
                  .translate((-126, sgn * LUG_Y, 110)))
    lugs = lug if lugs is None else lugs.union(lug)

# ---------------------------------------------------------------------------
# Feet under the body
# ---------------------------------------------------------------------------
feet = None
for sgn in (-1, 1):
    yc_ = sgn * Y0
    # skid plate along the bottom of each duct
    f = box(X_REAR + 2, X_FRONT - 8, yc_ - 40, yc_ + 40, -154, -124)
    # rear foot: tapered gusset plate
    f = f.union(xz_prism([(-198, -130), (-146, -130), (-178, FOOT_Z), (-194, FOOT_Z)],
                         yc_ - 12, yc_ + 12))
    # front foot: wide bracket block receiving the lower guard tube + gusset
    ya_, yb_ = sorted((sgn * 76, sgn * 150))
    f = f.union(xz_prism([(104, -118), (188, -118), (188, -206), (150, -206)], ya_, yb_))
    f = f.union(xz_prism([(150, -150), (188, -150), (188, FOOT_Z), (172, FOOT_Z)],
                         yc_ - 12, yc_ + 12))
    feet = f if feet is None else feet.union(f)
# small clip bracket with holes on the -Y side, rear
clip_br = box(-132, -92, -Y0 - 62, -Y0 - 34, -188, -110)
clip_br = clip_br.cut(cq.Workplane("XZ", origin=(0, -Y0 - 48, 0))
                      .pushPoints([(-112, -150), (-112, -172)]).circle(5)
                      .extrude(20, both=True))
feet = feet.union(clip_br)

# ---------------------------------------------------------------------------
# Guards
# ---------------------------------------------------------------------------
GY_UP = 200.0
rear_upper = pipe([(-170, -GY_UP, 250), (-448, -GY_UP, 106),
                   (-448, GY_UP, 106), (-170, GY_UP, 250)], bend=60)
GY_LO = 116.0
rear_lower = pipe([(-175, -GY_LO, -200), (-345, -GY_LO, -186), (-502, -GY_LO, 92),
                   (-502, GY_LO, 92), (-345, GY_LO, -186), (-175, GY_LO, -200)],
                  bend=70)

GY_F = 222.0
LEG_Y = 113.0
ARCH_Z = 64.0
arch = pipe([(414, -GY_F, -196), (304, -GY_F, ARCH_Z), (304, GY_F, ARCH_Z),
             (414, GY_F, -196)], bend=80)
cross = pipe([(374, -GY_F, -104), (374, GY_F, -104)])
stub = pipe([(200, 0, ARCH_Z), (306, 0, ARCH_Z)])
bottom = pipe([(414, -GY_F, -196), (262, -150, -198), (262, 150, -198),
               (414, GY_F, -196)], bend=60)
legs = None
for sgn in (-1, 1):
    lg = pipe([(170, sgn * LEG_Y, -184), (272, sgn * LEG_Y, -184)], bore=11.0)
    legs = lg if legs is None else legs.union(lg)

guards = (rear_upper.union(rear_lower).union(arch).union(cross)
          .union(stub).union(bottom).union(legs))

# ---------------------------------------------------------------------------
result = (body.union(cradle).union(drum).union(rails).union(saddle)
          .union(lugs).union(feet).union(guards))

VIEW = {"azimuth": 45, "elevation": 26}
